import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 900.0      # plate length (X)
PLATE_W = 120.0      # plate width (Y)
PLATE_T = 7.5        # plate thickness (Z)

BLOCK_X = 43.0       # end block size along X
BLOCK_Y = 73.5       # end block size along Y
BLOCK_H = 20.8       # end block height (sits on the plate)
BLOCK_FILLET = 1.5   # edge rounding of the blocks
BLOCK_END_OFFSET = 22.5   # block centre distance from plate end
BLOCK_PAT_END_OFFSET = 23.0  # hole pattern under the block, distance from plate end

CLUSTER_END_OFFSET = 97.5  # inboard hole cluster centre distance from plate end

# 8-hole mounting pattern (two overlapping rectangles) + centre hole
PAT_A = (15.25, 30.25)   # half spacing X, Y (also used by the block holes)
PAT_B = (7.75, 37.75)   # half spacing X, Y
HOLE_D = 4.0
CENTER_HOLE_D = 5.0
BLOCK_HOLE_D = 4.0
BLOCK_CSK_D = 7.0
BLOCK_CSK_ANGLE = 90.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
plate = cq.Workplane("XY").box(PLATE_L, PLATE_W, PLATE_T, centered=(True, True, False))


def pattern_pts(cx):
    pts = []
    for sx in (-1, 1):
        for sy in (-1, 1):
            pts.append((cx + sx * PAT_A[0], sy * PAT_A[1]))
            pts.append((cx + sx * PAT_B[0], sy * PAT_B[1]))
    return pts


cluster_centres = []
for side in (-1, 1):
    cluster_centres.append(side * (PLATE_L / 2 - CLUSTER_END_OFFSET))
    cluster_centres.append(side * (PLATE_L / 2 - BLOCK_PAT_END_OFFSET))

small_pts = []
for cx in cluster_centres:
    small_pts += pattern_pts(cx)

plate = (
    plate.faces(">Z").workplane(origin=(0, 0, PLATE_T))
    .pushPoints(small_pts).hole(HOLE_D)
)
plate = (
    plate.faces(">Z").workplane(origin=(0, 0, PLATE_T))
    .pushPoints([(cx, 0) for cx in cluster_centres]).hole(CENTER_HOLE_D)
)

# ---------------- end blocks (separate bodies resting on the plate) ----------------
bodies = [plate.val()]
for side in (-1, 1):
    bx = side * (PLATE_L / 2 - BLOCK_END_OFFSET)
    px = side * (PLATE_L / 2 - BLOCK_PAT_END_OFFSET)   # screw pattern centre
    blk = (
        cq.Workplane("XY")
        .box(BLOCK_X, BLOCK_Y, BLOCK_H, centered=(True, True, False))
        .edges().fillet(BLOCK_FILLET)
        .translate((bx, 0, PLATE_T))
    )
    blk = (
        blk.faces(">Z").workplane(origin=(px, 0, PLATE_T + BLOCK_H))
        .rect(2 * PAT_A[0], 2 * PAT_A[1], forConstruction=True)
        .vertices().cskHole(BLOCK_HOLE_D, BLOCK_CSK_D, BLOCK_CSK_ANGLE)
    )
    bodies.append(blk.val())

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(bodies)])
